import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R1 = 18.3          # radius of the rear (box) section == box height
R2 = 15.0          # main barrel radius
LB = 37.45         # box length
LT = 6.3           # box -> barrel transition cone length
RF1, RF2 = 3.0, 3.0  # blend radii at both ends of the transition
YC = 98.2          # start of the front cone
LC = 16.8          # front cone length
RCE = 8.2          # radius at end of front cone
RTIP = 6.25        # tip spigot radius
LTIP = 6.35        # tip spigot length
T = 2.5            # general wall thickness
TT = 1.3           # tip spigot wall thickness
TF = 2.6           # front (cable end) wall thickness
LTOT = YC + LC + LTIP

# barrel vent ring (9 slots + 2 half slots on the split line)
VENT_Y = 91.7      # centre of vent slots along the axis
VENT_L = 4.4       # slot length (axial)
VENT_W = 1.35      # slot width (tangential)
VENT_STEP = 18.0   # angular pitch (deg)
VENT_DEPTH = 3.2   # radial depth of the vent recess

# thick bulkhead behind the vent ring
BH_Y0, BH_Y1 = 87.0, 94.2
BH_HOLE = 1.5
BH_CH_X = 4.5      # wire channels through the bulkhead (x = +/-)
BH_CH_R = 1.0
# inner guide tube reaching back from the spigot into the front cone
IT_Y0 = 109.5

# rear (box) vents on the rounded -X side
BV_Y0, BV_Y1 = 5.9, 15.6
BV_ANGLES = [45, 52, 59, 66, 73, 80]   # measured from +Z towards -X
BV_W = 1.3

# front notch (cable entry)
FN_X0, FN_X1 = -13.9, -5.7
FN_H = 5.7

# side arch on +X wall
ARCH_Y = 12.7
ARCH_R = 6.4

# small notch on -X split edge of box
SN_Y0, SN_Y1 = 20.0, 24.2
SN_H = 3.5

# annular rib at barrel entry
AR_RIN = 10.0
AR_W = 1.5

# notch on -X split edge of front cone
CN_R = 3.3
CN_Z = -0.7
CN_Y = 110.0

BIG = 400.0


def revolve_profile(pts, radii=None):
    """Revolve a closed (r, y) polygon 360 deg about the Y axis.
    radii: optional {vertex index: fillet radius} to round profile corners."""
    radii = radii or {}
    n = len(pts)
    wp = cq.Workplane("XY")
    segs = []
    for i, p in enumerate(pts):
        r = radii.get(i, 0.0)
        if r <= 0:
            segs.append(("pt", p))
            continue
        a, b = pts[i - 1], pts[(i + 1) % n]
        u1 = ((a[0] - p[0]), (a[1] - p[1]))
        u2 = ((b[0] - p[0]), (b[1] - p[1]))
        l1, l2 = math.hypot(*u1), math.hypot(*u2)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (u2[0] / l2, u2[1] / l2)
        cosang = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        ang = math.acos(cosang)            # interior angle at the corner
        d = r / math.tan(ang / 2)
        t1 = (p[0] + u1[0] * d, p[1] + u1[1] * d)
        t2 = (p[0] + u2[0] * d, p[1] + u2[1] * d)
        bis = (u1[0] + u2[0], u1[1] + u2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        h = r / math.sin(ang / 2)
        c = (p[0] + bis[0] * h, p[1] + bis[1] * h)
        m = (c[0] - bis[0] * r, c[1] - bis[1] * r)
        segs.append(("arc", t1, m, t2))
    first = segs[0][1]
    wp = wp.moveTo(*first)
    for sgi in segs[1:]:
        if sgi[0] == "pt":
            wp = wp.lineTo(*sgi[1])
        else:
            wp = wp.lineTo(*sgi[1]).threePointArc(sgi[2], sgi[3])
    wp = wp.close()
    return wp.revolve(360, (0, 0, 0), (0, 1, 0))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_x(r, x0, x1, y, z):
    """Cylinder along X (seam rotated away from the split plane)."""
    s = cq.Solid.makeCylinder(r, x1 - x0, cq.Vector(x0, y, z), cq.Vector(1, 0, 0))
    s = s.rotate(cq.Vector(x0, y, z), cq.Vector(x1, y, z), 45)
    return cq.Workplane("XY").add(s)


def ring(r_out, r_in, y0, y1):
    s = cq.Solid.makeCylinder(r_out, y1 - y0, cq.Vector(0, y0, 0), cq.Vector(0, 1, 0))
    if r_in > 0:
        s = s.cut(cq.Solid.makeCylinder(r_in, y1 - y0, cq.Vector(0, y0, 0), cq.Vector(0, 1, 0)))
    s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 45)
    return cq.Workplane("XY").add(s).intersect(upper)


upper = box(-BIG, BIG, -BIG, BIG, 0, BIG)

# ---------------- outer body ----------------
outer_pts = [
    (0, 0), (R1, 0), (R1, LB), (R2, LB + LT), (R2, YC),
    (RCE, YC + LC), (RTIP, YC + LC), (RTIP, LTOT), (0, LTOT),
]
outer = revolve_profile(outer_pts, {2: RF1, 3: RF2})
outer = outer.union(box(0, R1, 0, LB, 0, R1))
outer = outer.intersect(upper)

# ---------------- inner cavity ----------------
inner_pts = [
    (0, TF), (R1 - T, TF), (R1 - T, LB + 0.5), (R2 - T, LB + LT + 0.5),
    (R2 - T, YC + 0.6), (RCE - T, YC + LC - 0.8), (RTIP - TT, YC + LC - 0.8),
    (RTIP - TT, LTOT + 1), (0, LTOT + 1),
]
cavity = revolve_profile(inner_pts)
cavity = cavity.union(box(0, R1 - T, TF, LB - T, -1, R1 - T))
body = outer.cut(cavity.intersect(box(-BIG, BIG, -BIG, BIG, -1, BIG)))

# ---------------- internal ribs ----------------
# annular rib at barrel entry
body = body.union(ring(R2 - T + 0.2, AR_RIN, LB + LT + 0.6, LB + LT + 0.6 + AR_W))
# thick bulkhead under the vent ring
body = body.union(ring(R2 - T + 0.2, BH_HOLE, BH_Y0, BH_Y1))

# guide tube continuing the spigot bore back into the cone
body = body.union(ring(RTIP, RTIP - TT, IT_Y0, YC + LC - 0.5))
# lip inside the tip
body = body.union(ring(RTIP - TT + 0.2, RTIP - TT - 1.0, LTOT - 1.6, LTOT - 0.7))
# raised rib just behind the front wall
rib_env = revolve_profile([(0, 0), (R1 - 0.2, 0), (R1 - 0.2, 10), (0, 10)]).union(
    box(0, R1 - 0.2, 0, 10, 0, R1 - 0.2))
rib = box(-R1, R1, TF - 0.1, TF + 2.0, 1.3, R1).intersect(rib_env)
body = body.union(rib)

# ---------------- cut features ----------------
# barrel vent ring (recessed into the bulkhead)
n = int(round(90 / VENT_STEP))
for i in range(-n, n + 1):
    ang = i * VENT_STEP
    slot = (cq.Workplane("XY")
            .box(VENT_W, VENT_L, VENT_DEPTH + 2)
            .translate((0, VENT_Y, R2 - VENT_DEPTH / 2 + 1))
            .rotate((0, 0, 0), (0, 1, 0), ang))
    body = body.cut(slot)

# rear vents on rounded -X side of the box
for a in BV_ANGLES:
    slot = (cq.Workplane("XY")
            .box(BV_W, BV_Y1 - BV_Y0, 2 * T + 4)
            .translate((0, (BV_Y0 + BV_Y1) / 2, R1))
            .rotate((0, 0, 0), (0, 1, 0), -a))
    body = body.cut(slot)

# wire channels along the split face of the bulkhead
for sx in (-BH_CH_X, BH_CH_X):
    ch = cq.Solid.makeCylinder(BH_CH_R, BH_Y1 - BH_Y0 + 2, cq.Vector(sx, BH_Y0 - 1, 0),
                               cq.Vector(0, 1, 0))
    ch = ch.rotate(cq.Vector(sx, 0, 0), cq.Vector(sx, 1, 0), 45)
    body = body.cut(cq.Workplane("XY").add(ch))

# front notch through front wall and rib
body = body.cut(box(FN_X0, FN_X1, -1, TF + 3.0, -1, FN_H))

# arch on +X wall
body = body.cut(cyl_x(ARCH_R, R1 - T - 1, R1 + 1, ARCH_Y, 0))

# small notch on -X split edge
body = body.cut(box(-R1 - 1, -R1 + T + 1, SN_Y0, SN_Y1, -1, SN_H))

# semicircular notch on -X side of front cone
rn = R2 - (R2 - RCE) * (CN_Y - YC) / LC
body = body.cut(cyl_x(CN_R, -rn - 3, -rn + T + 1, CN_Y, CN_Z))

result = body
